"""Studded cup: a cylindrical cup with a blind bore, ringed by 40 faceted beads
(20 staggered columns x 2 beads, on 4 rows) set into the outer wall."""
import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
OUTER_D = 62.0          # outer diameter of the cup body
HEIGHT = 40.0           # overall height of the cup body
WALL = 4.4              # side wall thickness
FLOOR = 4.4             # bottom thickness (blind bore from the top)

N_COLS = 20             # stud columns around the circumference
ROW_PITCH = HEIGHT / 6.0
ROW_Z = [ROW_PITCH * i for i in (1, 2, 3, 4)]   # stud row heights (bottom -> top)
COL0_ANGLE = -90.0      # column 0 faces the front (-Y); even columns hold rows 2 & 4 from the bottom,
                        # odd columns rows 1 & 3 (staggered pattern)

# faceted bead (12 facets around a vertical axis, one vertex pointing outward)
BEAD_SEG = 12
BEAD_A = 7.47           # circumradius of the equator polygon (tangential)
BEAD_K = 1.25           # radial elongation of the bead
BEAD_SINK = 6.04        # bead centre lies this far inside the outer surface
BAND_LAT = 31.0         # facet band reaches this "latitude" (z = A*sin) before the caps
FACET_DRAFT = 18.0      # inclination of the band facets (deg from the bead axis)
CAP_SLOPE = 37.5        # slope of the conical caps (deg from horizontal)

R = OUTER_D / 2.0


def equator_wire(a, k):
    """Equator polygon of the bead, one vertex on +X (radial), radial axis scaled by k."""
    pts = [cq.Vector(k * a * math.cos(2.0 * math.pi * i / BEAD_SEG),
                     a * math.sin(2.0 * math.pi * i / BEAD_SEG), 0.0)
           for i in range(BEAD_SEG)]
    return cq.Wire.makePolygon(pts, close=True)


def facet_frustum(a, k, below, above):
    """Drafted extrusion of the equator polygon: its planar faces are the
    upper facet band of the bead (section at z=0 is the equator polygon)."""
    grow = below * math.tan(math.radians(FACET_DRAFT))
    base = equator_wire(a, k).offset2D(grow, "intersection")[0]
    base = base.translate(cq.Vector(0, 0, -below))
    return cq.Solid.extrudeLinear(cq.Face.makeFromWires(base),
                                  cq.Vector(0, 0, below + above), taper=FACET_DRAFT)


def cap_cone(a, k, below):
    """Conical cap passing through the front corners of the facet band top."""
    z1 = a * math.sin(math.radians(BAND_LAT))
    top = equator_wire(a, k).offset2D(-z1 * math.tan(math.radians(FACET_DRAFT)),
                                      "intersection")[0]
    vs = [v.toTuple() for v in top.Vertices()]
    p0 = max(vs, key=lambda p: p[0] - 10.0 * abs(p[1]))          # outward corner
    p1 = max((p for p in vs if p[1] > 1e-6), key=lambda p: p[0])  # next corner
    # circle (centre on the radial axis) through p0 and the two neighbours
    x0 = (p0[0] ** 2 - p1[0] ** 2 - p1[1] ** 2) / (2.0 * (p0[0] - p1[0]))
    r1 = p0[0] - x0
    run = 1.0 / math.tan(math.radians(CAP_SLOPE))
    zt = z1 + 0.95 * r1 / run
    rt = r1 - (zt - z1) * run
    rb = r1 + (z1 + below) * run
    return cq.Solid.makeCone(rb, rt, zt + below, cq.Vector(x0, 0, -below), cq.Vector(0, 0, 1))


def bead(a, k):
    """Faceted bead: 12-sided double frustum band with conical caps top and bottom."""
    below, above = 1.0 * a, 1.3 * a
    up = facet_frustum(a, k, below, above)
    cone = cap_cone(a, k, below)
    return (up.intersect(up.mirror("XY"))
              .intersect(cone)
              .intersect(cone.mirror("XY")))


# ---------------- body ----------------
ORIGIN, Z_AXIS = cq.Vector(0, 0, 0), cq.Vector(0, 0, 1)
# (the cylinders are turned so their seam lines sit where they are least visible)
body = cq.Workplane("XY").circle(R).extrude(HEIGHT).val().rotate(ORIGIN, Z_AXIS, 90)

# one stud: bead sunk into the wall, trimmed to the part outside the body
# (identical for every position because the body is a surface of revolution)
core = cq.Solid.makeCylinder(R, 4.0 * BEAD_A, cq.Vector(0, 0, -2.0 * BEAD_A))
stud = bead(BEAD_A, BEAD_K).translate(cq.Vector(R - BEAD_SINK, 0, 0)).cut(core)

studs = []
for col in range(N_COLS):
    ang = COL0_ANGLE + col * 360.0 / N_COLS
    rows = (ROW_Z[3], ROW_Z[1]) if col % 2 == 0 else (ROW_Z[2], ROW_Z[0])
    for z in rows:
        studs.append(stud.translate(cq.Vector(0, 0, z)).rotate(ORIGIN, Z_AXIS, ang))

body = body.fuse(*studs)

# blind bore from the top
bore = (cq.Workplane("XY").workplane(offset=FLOOR).circle(R - WALL).extrude(HEIGHT).val()
        .rotate(ORIGIN, Z_AXIS, 45))
result = cq.Workplane("XY").add(body.cut(bore).clean())

VIEW = {"azimuth": 45, "elevation": 26}
